"""Rounded end block with a side groove, end bore and an elliptical pocket.

Orientation (as in the reference renders):
  X : length, the big rounded plan corner sits at (+X, -Y)
  Y : width,  the flat +Y face carries a part-round groove running along X
  Z : height, part sits on z = 0
"""
import cadquery as cq

try:  # multi-radius fillet builder (OCCT, shipped with cadquery)
    from cadquery.occ_impl.shapes import BRepFilletAPI_MakeFillet
except ImportError:  # pragma: no cover
    from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
L = 86.0          # length along X
W = 43.0          # width along Y
H = 20.0          # height along Z

R_BIG = 20.0      # big vertical (plan) corner radius at (+X,-Y)
R_NEG = 1.7       # small vertical corner radius at (-X,-Y)

R_EDGE = 5.2      # top / bottom perimeter round (-Y side, big corner, +X end)
R_EDGE_X = 4.4    # top / bottom round along the -X end
                  # (edges along the flat +Y face stay sharp)

# part-round groove along X in the flat +Y face (runs the full length)
CH_R = 7.83       # groove radius
CH_OFF = 2.93     # groove axis lies this far outside the +Y face
                  # -> chord 14.5, depth 4.9, 2.75 mm lands top and bottom

# blind bore in the -X end face (along +X)
BORE_D = 15.0
BORE_Y = -4.5     # bore axis y (part centred on y = 0)
BORE_Z = H / 2
BORE_DEPTH = 30.0

# elliptical pocket sunk into the groove floor (along -Y)
PK_LEN = 18.8     # pocket length along X
PK_W = 11.8       # pocket height along Z
PK_X = 19.1       # pocket centre x (part centred on x = 0)
PK_Z = H / 2      # pocket centre z
PK_DEPTH = 14.5   # depth below the groove floor

VIEW = {"azimuth": 45, "elevation": 26}

EPS = 1e-3

# ---------------- base block with the plan-view corners ----------------
base = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))
base = base.edges("|Z and >X and <Y").fillet(R_BIG)
base = base.edges("|Z and <X and <Y").fillet(R_NEG)

# ---------------- top / bottom perimeter rounds ----------------
# one fillet operation, two radii: smaller along the -X end,
# none along the flat +Y face
solid = base.val()
mk = BRepFilletAPI_MakeFillet(solid.wrapped)
for e in solid.Edges():
    bb = e.BoundingBox()
    if bb.zlen > EPS:
        continue                                   # vertical edges
    zc = 0.5 * (bb.zmin + bb.zmax)
    if abs(zc) > EPS and abs(zc - H) > EPS:
        continue                                   # not on top / bottom
    if bb.ymin > W / 2 - EPS:
        continue                                   # +Y edges stay sharp
    r = R_EDGE_X if bb.xmax < -L / 2 + EPS else R_EDGE
    mk.Add(r, e.wrapped)
mk.Build()
body = cq.Workplane("XY").newObject([cq.Shape.cast(mk.Shape())])

# ---------------- groove along the +Y face ----------------
groove = (
    cq.Workplane("YZ", origin=(-L / 2 - 1, 0, 0))
    .center(W / 2 + CH_OFF, H / 2)
    .circle(CH_R)
    .extrude(L + 2)
)
body = body.cut(groove)

# ---------------- blind bore in the -X end ----------------
bore = (
    cq.Workplane("YZ", origin=(-L / 2 - 1, 0, 0))
    .center(BORE_Y, BORE_Z)
    .circle(BORE_D / 2)
    .extrude(BORE_DEPTH + 1)
)
body = body.cut(bore)

# ---------------- elliptical pocket in the groove floor ----------------
groove_floor_y = W / 2 + CH_OFF - CH_R
pocket = (
    cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))   # XZ normal is -Y
    .center(PK_X, PK_Z)
    .ellipse(PK_LEN / 2, PK_W / 2)
    .extrude(W / 2 + 1 - groove_floor_y + PK_DEPTH)
)
body = body.cut(pocket)

result = body
